import math
import cadquery as cq

# =====================================================================
# Flanged motor cup with rear mounting tab (nut traps) - parametric
# Cup axis = Y.  Flange face at -Y (front), back wall + tab at +Y.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 90.0        # front mounting flange diameter
FLANGE_T = 12.0        # flange thickness
BODY_D = 78.0          # cup body outer diameter
TOTAL_L = 50.0         # overall length along Y (flange face to back face)
BORE_D = 66.0          # cup bore diameter
BACK_T = 10.0          # back wall / mounting tab thickness
FLANGE_FILLET = 5.0    # fillet between flange back face and body

TAB_W = 66.0           # mounting tab width
TAB_BOTTOM = 75.0      # tab bottom edge below cup axis
TAB_CORNER_R = 12.0    # tab bottom corner radius
TAB_JOIN_R = 20.0      # concave blend between cup outline and tab sides

FL_HOLE_D = 6.0        # flange blind (tap-drill) holes
FL_HOLE_BC = 78.0      # flange bolt circle diameter
FL_HOLE_DEPTH = 10.0   # full-diameter depth
FL_HOLE_N = 4
DRILL_ANGLE = 118.0    # drill point angle of blind holes

BACK_CENTER_D = 9.5    # centre hole in back wall
BACK_RING_R = 19.0     # radius of hole ring in back wall
BACK_RING_D = 9.5      # six large holes (0, 60, ... deg)
BACK_SMALL_D = 3.5     # three small holes (90, 210, 330 deg)

NUT_HOLE_D = 4.6       # tab bolt through holes
NUT_AC = 9.7           # hex nut pocket across corners
NUT_DEPTH = 4.0        # hex pocket depth (from tab front face)
NUT_POS = [(0.0, -48.0), (-22.3, -64.7), (22.3, -64.7)]  # (x, z)

CABLE_R = 8.5          # half-round cable exit through cup floor at back wall

# cosmetic only: angular position (deg, in XZ from +X toward +Z) of cylinder seams,
# chosen so seam edges sit where they are not seen from the usual viewpoints
SEAM_OUTER = 230.0     # outside of flange / body
SEAM_INNER = 0.0       # bore (concave)
SEAM_HOLE = 45.0       # holes

# ---------------- derived positions ----------------
y_front = -TOTAL_L / 2.0
y_back = TOTAL_L / 2.0
y_flange_back = y_front + FLANGE_T
y_wall = y_back - BACK_T          # inner face of back wall == front face of tab


def _seam(shape, x, z, seam_deg):
    """Spin a Y-axis solid of revolution about its own axis to place its seam."""
    return shape.rotate(cq.Vector(x, 0, z), cq.Vector(x, 1, z), 90.0 - seam_deg)


def ycyl(r, y0, y1, x=0.0, z=0.0, seam_deg=SEAM_HOLE):
    """Solid cylinder along +Y from y0 to y1, centred at (x, z)."""
    s = cq.Solid.makeCylinder(r, y1 - y0, cq.Vector(x, y0, z), cq.Vector(0, 1, 0))
    return cq.Workplane("XY").add(_seam(s, x, z, seam_deg))


def blind_hole(r, y_start, depth, x, z, point_angle=DRILL_ANGLE):
    """Drilled blind hole along +Y with a conical drill point."""
    tip_h = r / math.tan(math.radians(point_angle / 2.0))
    cyl = cq.Solid.makeCylinder(r, depth, cq.Vector(x, y_start, z), cq.Vector(0, 1, 0))
    cone = cq.Solid.makeCone(r, 0.0, tip_h, cq.Vector(x, y_start + depth, z), cq.Vector(0, 1, 0))
    cyl = _seam(cyl, x, z, SEAM_HOLE)
    cone = _seam(cone, x, z, SEAM_HOLE)
    return cq.Workplane("XY").add(cyl).union(cq.Workplane("XY").add(cone))


# ---------------- main body ----------------
flange = ycyl(FLANGE_D / 2, y_front, y_flange_back, seam_deg=SEAM_OUTER)
body = ycyl(BODY_D / 2, y_flange_back, y_back, seam_deg=SEAM_OUTER)

tab = (
    cq.Workplane("XY")
    .box(TAB_W, BACK_T, TAB_BOTTOM, centered=(True, False, False))
    .translate((0, y_wall, -TAB_BOTTOM))
    .edges("|Y and <Z")
    .fillet(TAB_CORNER_R)
)

part = flange.union(body).union(tab)

# concave blends where the tab sides run into the round cup outline
z_join = -((BODY_D / 2) ** 2 - (TAB_W / 2) ** 2) ** 0.5
for sx in (-1, 1):
    part = part.edges(
        cq.selectors.NearestToPointSelector((sx * TAB_W / 2, (y_wall + y_back) / 2, z_join))
    ).fillet(TAB_JOIN_R)

# fillet between flange back face and body
part = part.edges(
    cq.selectors.BoxSelector((-BODY_D / 2 - 0.5, y_flange_back - 0.5, -BODY_D / 2 - 0.5),
                             (BODY_D / 2 + 0.5, y_flange_back + 0.5, BODY_D / 2 + 0.5),
                             boundingbox=True)
).fillet(FLANGE_FILLET)

# ---------------- cup bore ----------------
part = part.cut(ycyl(BORE_D / 2, y_front - 1, y_wall, seam_deg=SEAM_INNER))

# ---------------- flange blind holes (polar pattern) ----------------
for i in range(FL_HOLE_N):
    a = math.radians(90 + i * 360.0 / FL_HOLE_N)
    part = part.cut(blind_hole(FL_HOLE_D / 2, y_front - 1, FL_HOLE_DEPTH + 1,
                               FL_HOLE_BC / 2 * math.cos(a), FL_HOLE_BC / 2 * math.sin(a)))

# ---------------- back wall hole pattern ----------------
back_cut = ycyl(BACK_CENTER_D / 2, y_wall - 1, y_back + 1)
for i in range(6):
    a = math.radians(i * 60.0)
    back_cut = back_cut.union(
        ycyl(BACK_RING_D / 2, y_wall - 1, y_back + 1,
             BACK_RING_R * math.cos(a), BACK_RING_R * math.sin(a)))
for i in range(3):
    a = math.radians(90 + i * 120.0)
    back_cut = back_cut.union(
        ycyl(BACK_SMALL_D / 2, y_wall - 1, y_back + 1,
             BACK_RING_R * math.cos(a), BACK_RING_R * math.sin(a)))
part = part.cut(back_cut)

# ---------------- tab bolt holes with hex nut traps ----------------
for (nx, nz) in NUT_POS:
    part = part.cut(ycyl(NUT_HOLE_D / 2, y_wall - 1, y_back + 1, nx, nz))
    hexp = (
        cq.Workplane("XZ", origin=(nx, y_wall + NUT_DEPTH, nz))
        .polygon(6, NUT_AC)            # corners left/right, flats top/bottom
        .extrude(NUT_DEPTH + 1.0)      # XZ normal is -Y: cuts from pocket floor forward
    )
    part = part.cut(hexp)

# ---------------- half-round cable exit in cup floor at the back wall ----------------
cable = (
    cq.Workplane("XY", origin=(0, 0, -BODY_D / 2 - 3))
    .moveTo(-CABLE_R, y_wall)
    .threePointArc((0, y_wall - CABLE_R), (CABLE_R, y_wall))
    .close()
    .extrude(BODY_D / 2 - BORE_D / 2 + 6)
)
part = part.cut(cable)

result = part
